import math
import cadquery as cq

# ---------------------------------------------------------------
# Four-piece kit (pet-feeder style): tall housing, D-plate ring,
# lid ring and a shallow bowl with an embossed paw print.
# All dimensions in millimetres.
# ---------------------------------------------------------------

# seam angle of every revolved / cylindrical face (kept on a silhouette)
SEAM = 225.0

# ---- placement of the four bodies (centres in XY) ----
POS_DRING = (0.0, 0.0)
POS_HOUSING = (111.4, -27.6)
POS_LID = (27.8, -111.2)
POS_BOWL = (136.75, -136.9)

# ---- housing (tall cylinder) ----
H_R_OUT = 54.75
H_WALL = 2.0
H_HEIGHT = 43.8
H_LEDGE_R = 48.2          # inner radius of the lower thick ring
H_LEDGE_H = 16.0          # height of the lower thick ring
H_PLATE_X = -24.9         # chord position of the D floor plate
H_PLATE_H = 8.8           # thickness of floor plate / bosses
H_BOSS_R = 18.1           # radius of the boss segments
H_BOSS_C = 46.8           # centre distance of boss circles
H_BOSS_HOLE_Y = 38.3
H_BOSS_HOLE_D = 6.2
H_BOSS_HOLE_CH = 1.1      # chamfer at top of boss hole
H_BOSS_CB_D = 13.8
H_BOSS_CB_DEPTH = 4.0
H_PLATE_HOLE_X = -29.2
H_PLATE_HOLE_DY = 4.3
H_PLATE_HOLE_D = 3.5
H_PLATE_CS_D = 9.0        # countersink (from below) diameter
H_POCKET_HALF = 10.5      # half width of the wall opening at -X
H_POCKET_X_IN = -46.9     # inner limit of the opening (cuts the ledge)
H_POCKET_TOP = 20.0       # top of the opening
H_DEEP_Y0 = -8.5          # narrower, deeper slot of the opening
H_DEEP_Y1 = 10.5
H_WIN_Z0 = 1.0            # outer (lowest) end of the ramped slot floor

# ---- D-plate ring ----
D_R_OUT = 51.7
D_WALL = 2.0
D_HEIGHT = 16.2
D_LEDGE_R = 44.4
D_LEDGE_H = 9.0
D_PLATE_X = 24.4
D_HOLE_X = 29.3
D_HOLE_DY = 4.2
D_HOLE_D = 3.5
D_CS_D = 9.6              # countersink (from top) diameter

# ---- lid ring ----
L_R_FLANGE = 55.1
L_FLANGE_H = 1.5
L_R_WALL_OUT = 52.6
L_WALL = 1.6
L_HEIGHT = 8.9
L_R_IN = 43.0
L_GROOVE_Z = 0.8          # floor of the U-channel
L_GROOVE_FILLET = 2.5     # fillet between outer wall and channel floor
L_LIP_R = 46.0            # outer radius of the inner lip
L_LIP_H = 3.6             # height of the inner lip
L_CH = 0.3                # small chamfers on the lip top
L_CH_BOT = 0.4            # chamfer on the bottom inner edge

# ---- bowl ----
B_R_OUT = 49.0
B_HEIGHT = 14.6
B_RIM = 2.1               # flat rim width on top
B_FLOOR = 1.8             # floor thickness
B_FLOOR_R = 35.0          # radius of flat floor (conical inner wall)
B_PAW_H = 0.6             # emboss height of the paw print
PAW_ROT = -5.0            # the toe pads are turned slightly clockwise
# outline of the heart-shaped main pad (hand drawn, slightly irregular)
HEART_PTS = [(0.2, 1.1), (4.3, 3.9), (8.1, 8.3), (10.7, 12.6), (11.3, 15.5),
             (10.0, 17.7), (6.3, 18.3), (2.6, 17.6), (-0.5, 16.4),
             (-3.8, 17.8), (-6.7, 18.3), (-9.3, 17.4), (-10.5, 14.8),
             (-9.7, 11.4), (-7.4, 7.6), (-3.9, 3.8)]
# toe pads: (x, y, width, length, tilt)
PAW_TOES = [(-12.2, 0.0, 8.0, 13.5, -15.0), (12.2, 0.0, 8.0, 13.5, 15.0),
            (-5.2, -10.2, 8.0, 14.0, -5.0), (5.2, -10.2, 8.0, 14.0, 5.0)]

Z = cq.Vector(0, 0, 1)
O = cq.Vector(0, 0, 0)


def cyl(r, h, x=0.0, y=0.0, z=0.0):
    """Vertical cylinder with its seam turned to the SEAM angle."""
    s = cq.Solid.makeCylinder(r, h, O, Z).rotate(O, Z, SEAM)
    return s.translate(cq.Vector(x, y, z))


def cone(r1, r2, h, x=0.0, y=0.0, z=0.0):
    s = cq.Solid.makeCone(r1, r2, h, O, Z).rotate(O, Z, SEAM)
    return s.translate(cq.Vector(x, y, z))


def box(x0, x1, y0, y1, z0, z1):
    return cq.Solid.makeBox(x1 - x0, y1 - y0, z1 - z0,
                            cq.Vector(x0, y0, z0))


def housing():
    body = cyl(H_R_OUT, H_HEIGHT).cut(cyl(H_R_OUT - H_WALL, H_HEIGHT + 1, z=-0.5))
    inner = cyl(H_R_OUT - H_WALL + 0.01, H_LEDGE_H)
    ledge = inner.cut(cyl(H_LEDGE_R, H_LEDGE_H + 1, z=-0.5))
    body = body.fuse(ledge)
    low = cyl(H_R_OUT - H_WALL + 0.01, H_PLATE_H)
    # D floor plate on -X side
    plate = box(-H_R_OUT - 1, H_PLATE_X, -H_R_OUT - 1, H_R_OUT + 1,
                0, H_PLATE_H).intersect(low)
    body = body.fuse(plate)
    # boss segments at +/-Y
    for s in (1, -1):
        boss = cyl(H_BOSS_R, H_PLATE_H, 0, s * H_BOSS_C).intersect(low)
        body = body.fuse(boss)
    # boss holes: counterbore from the top, chamfered through hole
    for s in (1, -1):
        y = s * H_BOSS_HOLE_Y
        body = body.cut(cyl(H_BOSS_HOLE_D / 2, H_PLATE_H + 1, 0, y, -0.5))
        body = body.cut(cyl(H_BOSS_CB_D / 2, H_BOSS_CB_DEPTH + 1, 0, y,
                            H_PLATE_H - H_BOSS_CB_DEPTH))
        zc = H_PLATE_H - H_BOSS_CB_DEPTH
        body = body.cut(cone(H_BOSS_HOLE_D / 2, H_BOSS_HOLE_D / 2 + H_BOSS_HOLE_CH,
                             H_BOSS_HOLE_CH + 0.001, 0, y, zc - H_BOSS_HOLE_CH))
    # plate holes with (overlapping) countersinks from below
    for s in (1, -1):
        y = s * H_PLATE_HOLE_DY
        body = body.cut(cyl(H_PLATE_HOLE_D / 2, H_PLATE_H + 1,
                            H_PLATE_HOLE_X, y, -0.5))
        hcs = (H_PLATE_CS_D - H_PLATE_HOLE_D) / 2
        body = body.cut(cone(H_PLATE_CS_D / 2 + 0.5, H_PLATE_HOLE_D / 2,
                             hcs + 0.5, H_PLATE_HOLE_X, y, -0.5))
    # rectangular opening through the wall at -X (upper part spans the
    # full width, a narrower slot continues down through the floor plate)
    x_far = -H_R_OUT - 2.0
    body = body.cut(box(x_far, H_POCKET_X_IN, -H_POCKET_HALF, H_POCKET_HALF,
                        H_PLATE_H, H_POCKET_TOP))
    # the narrower slot has a floor ramping down towards the outside
    ramp = (cq.Workplane("XZ")
            .polyline([(H_POCKET_X_IN, H_PLATE_H + 0.01),
                       (H_POCKET_X_IN, H_PLATE_H),
                       (-H_R_OUT, H_WIN_Z0),
                       (x_far, H_WIN_Z0),
                       (x_far, H_PLATE_H + 0.01)]).close()
            .extrude(-(H_DEEP_Y1 - H_DEEP_Y0)).val()
            .translate(cq.Vector(0, H_DEEP_Y0, 0)))
    body = body.cut(ramp)
    return body


def d_ring():
    body = cyl(D_R_OUT, D_HEIGHT).cut(cyl(D_R_OUT - D_WALL, D_HEIGHT + 1, z=-0.5))
    inner = cyl(D_R_OUT - D_WALL + 0.01, D_LEDGE_H)
    ledge = inner.cut(cyl(D_LEDGE_R, D_LEDGE_H + 1, z=-0.5))
    body = body.fuse(ledge)
    plate = box(D_PLATE_X, D_R_OUT + 1, -D_R_OUT - 1, D_R_OUT + 1,
                0, D_LEDGE_H).intersect(inner)
    body = body.fuse(plate)
    for s in (1, -1):
        y = s * D_HOLE_DY
        body = body.cut(cyl(D_HOLE_D / 2, D_LEDGE_H + 1, D_HOLE_X, y, -0.5))
        hcs = (D_CS_D - D_HOLE_D) / 2
        body = body.cut(cone(D_HOLE_D / 2, D_CS_D / 2 + 0.5, hcs + 0.5,
                             D_HOLE_X, y, D_LEDGE_H - hcs))
    return body


def lid_ring():
    c = L_CH
    b = L_CH_BOT
    f = L_GROOVE_FILLET
    r_wi = L_R_WALL_OUT - L_WALL
    # fillet between the outer wall and the channel floor (arc midpoint)
    m = (r_wi - f + f * math.cos(math.radians(45)),
         L_GROOVE_Z + f - f * math.sin(math.radians(45)))
    wp = (cq.Workplane("XZ")
          .moveTo(L_R_IN + b, 0.0)
          .lineTo(L_R_FLANGE, 0.0)
          .lineTo(L_R_FLANGE, L_FLANGE_H)
          .lineTo(L_R_WALL_OUT, L_FLANGE_H)
          .lineTo(L_R_WALL_OUT, L_HEIGHT)
          .lineTo(r_wi, L_HEIGHT)
          .lineTo(r_wi, L_GROOVE_Z + f)
          .threePointArc(m, (r_wi - f, L_GROOVE_Z))
          .lineTo(L_LIP_R, L_GROOVE_Z)
          .lineTo(L_LIP_R, L_LIP_H - c)
          .lineTo(L_LIP_R - c, L_LIP_H)
          .lineTo(L_R_IN + c, L_LIP_H)
          .lineTo(L_R_IN, L_LIP_H - c)
          .lineTo(L_R_IN, b)
          .close())
    s = wp.revolve(360, (0, 0, 0), (0, 1, 0)).val()
    return s.rotate(O, Z, SEAM)


def heart_solid(z0, h):
    """Heart-shaped main pad: smooth periodic spline through HEART_PTS."""
    w = (cq.Workplane("XY").workplane(offset=z0)
         .spline(HEART_PTS, periodic=True).close())
    return w.extrude(h).val()


def bowl():
    body = cyl(B_R_OUT, B_HEIGHT)
    # conical cavity, its seam turned to the near side (hidden by the rim)
    h = B_HEIGHT - B_FLOOR
    r_top = B_R_OUT - B_RIM
    cav = (cq.Solid.makeCone(B_FLOOR_R, r_top, h, O, Z)
           .rotate(O, Z, SEAM + 90.0).translate(cq.Vector(0, 0, B_FLOOR)))
    cav = cav.fuse(cq.Solid.makeCylinder(r_top, 2.0, O, Z)
                   .rotate(O, Z, SEAM + 90.0)
                   .translate(cq.Vector(0, 0, B_HEIGHT - 0.001)))
    body = body.cut(cav)
    paw = heart_solid(B_FLOOR - 0.01, B_PAW_H + 0.01)
    for (tx, ty, w, hh, ang) in PAW_TOES:
        t = (cq.Workplane("XY").workplane(offset=B_FLOOR - 0.01)
             .ellipse(w / 2, hh / 2).extrude(B_PAW_H + 0.01).val()
             .rotate(O, Z, ang)
             .translate(cq.Vector(tx, ty, 0))
             .rotate(O, Z, PAW_ROT))
        paw = paw.fuse(t)
    return body.fuse(paw)


def place(shape, pos):
    return shape.translate(cq.Vector(pos[0], pos[1], 0))


parts = [
    place(housing().clean(), POS_HOUSING),
    place(d_ring().clean(), POS_DRING),
    place(lid_ring().clean(), POS_LID),
    place(bowl().clean(), POS_BOWL),
]
result = cq.Workplane("XY").add(cq.Compound.makeCompound(parts))

VIEW = {"azimuth": 45, "elevation": 26}
